import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 40.0          # overall width  (X)
L = 148.0         # overall length (Y)
H = 21.4          # overall height (Z)
T = 3.2           # wall thickness
FLOOR = 4.35      # floor top height

SHELF_Z = 15.4    # top of the inner longitudinal shelves
SHELF_A = 3.4     # shelf width in the -Y half
SHELF_B = 6.0     # shelf width in the +Y half

CH_Y0 = -3.35     # cross channel (middle, full inner width) start
CH_Y1 = 17.2      # cross channel end
CH_LINER = 0.5    # thin wall liner left along the side walls in the cross channel

# stepped blocks on the -Y side of the cross channel
BLK_X_IN = 6.1
BLK_LOW_Y0, BLK_STEP_Y = -10.3, -5.6
BLK_LOW_Z, BLK_HIGH_Z = 10.3, 12.4

# tooth + low pad on the +Y side of the cross channel
TOOTH_X_IN = 7.2
TOOTH_Y1 = 20.0
PAD_Y1 = 25.9
TOOTH_Z = 12.4
PAD_Z = 6.6

# guide blocks at the -Y end wall
END_X_IN = 6.0
END_DEPTH = 2.6
END_Z = 10.3

# raised pad at the +Y end + obround slot through the +Y wall
PADY_Y0 = 55.4
PADY_Z = 6.6
SLOT_Y0 = 59.9
SLOT_X0, SLOT_X1 = -12.2, 13.2   # slot ends (X)
SLOT_R = 3.75
SLOT_ZC = 6.95

# window in the -Y wall
WIN_W = 12.0
WIN_Z0, WIN_Z1 = 4.35, 11.76

# square hole in the floor
SQ_X0, SQ_X1 = -10.6, 0.4
SQ_Y0, SQ_Y1 = 37.5, 48.7

# transverse bore
BORE_Y = 6.6
BORE_Z = 7.3
BORE_D_BIG = 12.0
BORE_BIG_END_X = -6.5
BORE_D_SMALL = 5.8

IX = W / 2 - T   # inner half width
IY = L / 2 - T   # inner half length


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def sym_x(x0, x1, y0, y1, z0, z1):
    """box plus its mirror about the YZ plane (x0, x1 are on the -X side)"""
    return box(x0, x1, y0, y1, z0, z1).union(box(-x1, -x0, y0, y1, z0, z1))


# outer shell with open top
body = box(-W / 2, W / 2, -L / 2, L / 2, 0, H)
body = body.cut(box(-IX, IX, -IY, IY, FLOOR, H + 1))

# longitudinal shelves
body = body.union(sym_x(-IX, -IX + SHELF_A, -IY, CH_Y0, FLOOR - 0.01, SHELF_Z))
body = body.union(sym_x(-IX, -IX + SHELF_B, CH_Y1, IY, FLOOR - 0.01, SHELF_Z))

# thin liner along the side walls inside the cross channel (up to shelf height)
body = body.union(sym_x(-IX - 0.01, -IX + CH_LINER, CH_Y0 - 0.01, CH_Y1 + 0.01, FLOOR - 0.01, SHELF_Z))

# stepped blocks at the -Y side of the cross channel
xa = -IX + SHELF_A
body = body.union(sym_x(xa - 0.01, -BLK_X_IN, BLK_LOW_Y0, BLK_STEP_Y, FLOOR - 0.01, BLK_LOW_Z))
body = body.union(sym_x(xa - 0.01, -BLK_X_IN, BLK_STEP_Y - 0.01, CH_Y0, FLOOR - 0.01, BLK_HIGH_Z))

# tooth + low pad at the +Y side of the cross channel
xb = -IX + SHELF_B
body = body.union(sym_x(xb - 0.01, -TOOTH_X_IN, CH_Y1, TOOTH_Y1, FLOOR - 0.01, TOOTH_Z))
body = body.union(sym_x(xb - 0.01, -TOOTH_X_IN, TOOTH_Y1 - 0.01, PAD_Y1, FLOOR - 0.01, PAD_Z))

# guide blocks against the -Y end wall
body = body.union(sym_x(xa - 0.01, -END_X_IN, -IY - 0.01, -IY + END_DEPTH, FLOOR - 0.01, END_Z))

# raised pad at the +Y end
body = body.union(box(-IX + SHELF_B - 0.01, IX - SHELF_B + 0.01, PADY_Y0, IY + 0.01, FLOOR - 0.01, PADY_Z))

# obround slot through the +Y wall, running back into the pad
slot = (cq.Workplane("XZ", origin=(0, 0, 0))
        .center((SLOT_X0 + SLOT_X1) / 2, SLOT_ZC)
        .slot2D(SLOT_X1 - SLOT_X0, 2 * SLOT_R, 0)
        .extrude(-(L / 2 + 1 - SLOT_Y0))
        .translate((0, SLOT_Y0, 0)))
body = body.cut(slot)

# rectangular window through the -Y wall
body = body.cut(box(-WIN_W / 2, WIN_W / 2, -L / 2 - 1, -IY + 0.5, WIN_Z0, WIN_Z1))

# square hole through the floor
body = body.cut(box(SQ_X0, SQ_X1, SQ_Y0, SQ_Y1, -1, FLOOR + 0.5))

# transverse bore: large counterbore from -X side, small through hole
axis_p0 = (0, BORE_Y, BORE_Z)
axis_p1 = (1, BORE_Y, BORE_Z)
big = (cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0))
       .center(BORE_Y, BORE_Z).circle(BORE_D_BIG / 2)
       .extrude(BORE_BIG_END_X - (-W / 2 - 1))
       .rotate(axis_p0, axis_p1, 90))          # put the seam on top
small = (cq.Workplane("YZ", origin=(-W / 2 - 1, 0, 0))
         .center(BORE_Y, BORE_Z).circle(BORE_D_SMALL / 2)
         .extrude(W + 2)                      # through the whole width
         .rotate(axis_p0, axis_p1, 90))
body = body.cut(big).cut(small)

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
